"""Wheel: round-crown tyre on a five spoke rim with a bored hub.

Wheel axis = global Y.  Everything is built from revolved profiles (tyre + rim),
extruded cylinders (hub, bore, holes) and boolean spokes.
"""
import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R_OUT = 100.0            # tyre outer radius
TIRE_HW = 19.3           # tyre half width at its widest point
CROWN_R = TIRE_HW        # full round crown (semicircle)
TIRE_ROOT_HW = 17.2      # tyre half width where it meets the rim (bulged side walls)
RIM_FACE_R = 63.2        # outer radius of the rim side face (step to the tyre)
RIM_HW = 20.0            # rim half width (flat side faces stand proud of the tyre)
RIM_BORE_R = 49.8        # radius of the rim opening at the side faces
RIM_LAND = 2.0           # short cylindrical land inside the opening
RIM_MIN_R = 39.3         # smallest radius of the rounded inner rim bead (mid plane)
BEAD_PT = (-10.0, 47.3)  # (axial, radial) point the S shaped inner rim profile passes

HUB_R = 23.2             # hub outer radius
HUB_HL = 25.2            # hub half length
BORE_R = 11.7            # through bore
CBORE_R = 14.4           # counterbore (bearing seat) at each hub end
CBORE_CH = 1.4           # chamfer at counterbore mouth
CBORE_D = 10.0           # counterbore depth
BOLT_PCD_R = 18.8        # radius of the 4 hole bolt circle on each hub face
BOLT_D = 4.4
BOLT_DEPTH = 8.0

N_SPOKES = 5
SPOKE_ANG = 15.0         # angular width of each (sector shaped) spoke
SPOKE_START = 180.0      # one spoke points to -X
SPOKE_Y_OUT = 10.0       # spoke half depth at the rim end (r = BEAD_PT radius)
SPOKE_TAPER = 0.274      # growth of spoke half depth per mm towards the hub


# ---------------- small 2D vector helpers ----------------
def _sub(a, b):
    return (a[0] - b[0], a[1] - b[1])


def _add(a, b):
    return (a[0] + b[0], a[1] + b[1])


def _mul(a, k):
    return (a[0] * k, a[1] * k)


def _dot(a, b):
    return a[0] * b[0] + a[1] * b[1]


def _norm(a):
    l = math.hypot(a[0], a[1])
    return (a[0] / l, a[1] / l)


def rp(p, s=1.0):
    """(axial y, radius r) -> sketch point (x = r, y = axial)"""
    return (p[1], s * p[0])


# ---------------- inner rim profile: concave arc + convex bead arc ----------------
P00 = (-RIM_HW, RIM_BORE_R)              # crease at the side face (y, r)
P0 = (-RIM_HW + RIM_LAND, RIM_BORE_R)    # start of the S curve, tangent axial
n0 = (0.0, -1.0)
d = _sub(BEAD_PT, P0)
rho1 = _dot(d, d) / (2 * _dot(d, n0))    # concave arc radius (through BEAD_PT)
C1 = _add(P0, _mul(n0, rho1))
_a = C1[0] ** 2 + (C1[1] - RIM_MIN_R) ** 2 - rho1 ** 2
rho2 = _a / (2 * (rho1 + (C1[1] - RIM_MIN_R)))   # convex bead radius
C2 = (0.0, RIM_MIN_R + rho2)
I = _add(C1, _mul(_sub(C2, C1), rho1 / (rho1 + rho2)))   # inflection (tangent) point
B = (0.0, RIM_MIN_R)
M1 = _add(C1, _mul(_norm(_add(_sub(P0, C1), _sub(I, C1))), rho1))
M2 = _add(C2, _mul(_norm(_add(_sub(I, C2), _sub(B, C2))), rho2))

# ---------------- tyre side wall: large arc tangent to the crown round ----------------
SW_R = ((R_OUT - CROWN_R - RIM_FACE_R) ** 2 + (TIRE_HW - TIRE_ROOT_HW) ** 2) / (2 * (TIRE_HW - TIRE_ROOT_HW))
SW_C = (R_OUT - CROWN_R, -TIRE_HW + SW_R)      # centre (r, y) of the front side wall arc
_v = _norm(_add(_sub((RIM_FACE_R, -TIRE_ROOT_HW), SW_C), _sub((R_OUT - CROWN_R, -TIRE_HW), SW_C)))
SW_M = (SW_C[0] + SW_R * _v[0], SW_C[1] + SW_R * _v[1])

# ---------------- tyre + rim: one revolved half section ----------------
prof = (
    cq.Workplane("XY")
    .moveTo(*rp(P00))
    .lineTo(RIM_FACE_R, -RIM_HW)                                  # front rim face
    .lineTo(RIM_FACE_R, -TIRE_ROOT_HW)                            # step to tyre
    .threePointArc(SW_M, (R_OUT - CROWN_R, -TIRE_HW))             # bulged side wall
    .threePointArc((R_OUT, 0), (R_OUT - CROWN_R, TIRE_HW))        # full round crown
    .threePointArc((SW_M[0], -SW_M[1]), (RIM_FACE_R, TIRE_ROOT_HW))
    .lineTo(RIM_FACE_R, RIM_HW)
    .lineTo(*rp(P00, -1))                                         # back rim face
    .lineTo(*rp(P0, -1))                                          # land
    .threePointArc(rp(M1, -1), rp(I, -1))                         # concave
    .threePointArc(rp(M2, -1), rp(B))                             # convex bead
    .threePointArc(rp(M2), rp(I))
    .threePointArc(rp(M1), rp(P0))
    .close()
)
# revolve about the wheel axis (Y); seam turned to the -X side (behind a spoke)
wheel = prof.revolve(360, (0, 0, 0), (0, 1, 0)).rotate((0, 0, 0), (0, 1, 0), 180)

# ---------------- hub ----------------
hub = (
    cq.Workplane("XZ").circle(HUB_R).extrude(HUB_HL, both=True)
    .rotate((0, 0, 0), (0, 1, 0), 180)
)


# ---------------- spokes: sector in the front view, tapered in the side view ----------------
def spoke(angle_deg):
    r_far = RIM_BORE_R + 4.0          # buried in the rim
    r_near = HUB_R - 6.0              # buried in the hub
    ha = math.radians(SPOKE_ANG / 2)
    wedge = (
        cq.Workplane("XZ")
        .polyline([(0, 0), (r_far * math.cos(ha), -r_far * math.sin(ha)),
                   (r_far * math.cos(ha), r_far * math.sin(ha))])
        .close()
        .extrude(HUB_HL, both=True)
    )

    def yf(r):
        return SPOKE_Y_OUT + SPOKE_TAPER * (BEAD_PT[1] - r)

    side = (
        cq.Workplane("XY")
        .polyline([(r_near, -yf(r_near)), (r_far, -yf(r_far)),
                   (r_far, yf(r_far)), (r_near, yf(r_near))])
        .close()
        .extrude(r_far, both=True)
    )
    # rotate about +Y by -angle so the spoke points at angle (from +X towards +Z)
    return wedge.intersect(side).rotate((0, 0, 0), (0, 1, 0), -angle_deg)


spokes = None
for i in range(N_SPOKES):
    s = spoke(SPOKE_START + i * 360.0 / N_SPOKES)
    spokes = s if spokes is None else spokes.union(s)

body = wheel.union(hub).union(spokes)

# ---------------- through bore, counterbores and bolt holes (both hub ends) ----------------
bore = cq.Workplane("XZ").circle(BORE_R).extrude(HUB_HL + 1, both=True)
body = body.cut(bore)
for sgn in (-1, 1):
    y_face = sgn * HUB_HL
    y_in = sgn * (HUB_HL - CBORE_D)
    y_out = sgn * (HUB_HL + 1)
    cbore = (
        cq.Workplane("XY")
        .polyline([(0, y_out), (CBORE_R + CBORE_CH + 1, y_out),
                   (CBORE_R + CBORE_CH + 1, y_face), (CBORE_R + CBORE_CH, y_face),
                   (CBORE_R, y_face - sgn * CBORE_CH), (CBORE_R, y_in), (0, y_in)])
        .close()
        .revolve(360, (0, 0, 0), (0, 1, 0))
    )
    body = body.cut(cbore)
    for k in range(4):
        a = math.radians(45 + 90 * k)
        hole = (
            cq.Workplane("XZ", origin=(BOLT_PCD_R * math.cos(a), y_out, BOLT_PCD_R * math.sin(a)))
            .circle(BOLT_D / 2)
            .extrude(-(BOLT_DEPTH + 1) if sgn < 0 else (BOLT_DEPTH + 1))
        )
        body = body.cut(hole)

result = body
